import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 118.0          # overall length (X)
H = 81.5           # overall height incl. end lobes (Z)
BODY_H = 64.0      # height of main body between the lobes (Z)
D = 17.0           # overall depth (Y); closed face at -Y, open at +Y
LOBE_W = 11.2      # width of the end bars / lobes (X)
LOBE_R = LOBE_W / 2.0
NECK_R = 3.0       # concave fillet between lobe and body top/bottom

WALL_TB = 2.2      # top / bottom wall thickness
WALL_XP = 2.2      # +X end wall thickness
WALL_XN = 1.6      # -X end wall thickness (thin part)
FLOOR = 2.2        # closed front wall thickness

BOT_CH = 2.3       # chamfer in the cavity's bottom +X corner

# corner post in the cavity's top +X corner (flush with the rim)
POST_W = 3.2       # width along X (its lower inner corner is chamfered 45 deg)
POST_Z0 = 27.4     # z where the post's inner face starts
# small triangular gusset beside the post, sunk below the rim
GUS_X = 5.0
GUS_Z = 3.0
GUS_SINK = 0.8

# thick section of the +X end wall (lower part)
BLOCK_T = 4.0      # extra thickness
BLOCK_TOP = -12.3  # z where the sloped transition starts
BLOCK_CH = 3.3     # vertical extent of the transition

# -X end wall: thick, with full-depth notches thinning it (z ranges)
RIB_T = 1.9        # depth of the notches (thick wall = WALL_XN + RIB_T)
NOTCHES_XN = [(-18.0, -8.0), (0.2, 9.4), (14.2, 26.7)]

HOLE_D = 3.0       # screw holes in the lobes
HOLE_CH = 0.4      # entry chamfer
HOLE_DEPTH = 14.0
HOLE_Z = H / 2.0 - LOBE_R

# internal standoffs (x, z)
BOSS_POS = [(17.3, 20.4), (16.7, -9.7), (43.6, -26.4), (-38.4, -26.3)]
BOSS_OD = 5.3
BOSS_ID = 2.2
BOSS_H = 3.7
BOSS_CH = 0.4

# port in the -X end face
PORT_Z = -12.8
PORT_OUT = (10.0, 13.9)   # recess (Y, Z)
PORT_OUT_R = 2.0
PORT_OUT_DEPTH = 0.8
PORT_IN = (4.2, 9.2)      # through opening (Y, Z)
PORT_IN_R = 1.0

# tiny triangular marks sunk into the front face at the -X cavity corners
MARK_LEG = 1.8
MARK_DEPTH = 1.0

# ---------------- outer shell ----------------
x_lobe = W / 2.0 - LOBE_R
body = cq.Workplane("XZ").rect(W, BODY_H).extrude(D / 2.0, both=True)
for sx in (1, -1):
    lobe = (
        cq.Workplane("XZ")
        .center(sx * x_lobe, 0)
        .slot2D(H, LOBE_W, angle=90)
        .extrude(D / 2.0, both=True)
    )
    body = body.union(lobe)

# concave fillets where lobes meet the body
xn = W / 2.0 - LOBE_W
for sx in (1, -1):
    body = body.edges(
        cq.selectors.BoxSelector(
            (sx * xn - 0.01, -D, -BODY_H / 2 - 0.01),
            (sx * xn + 0.01, D, BODY_H / 2 + 0.01),
        )
    ).fillet(NECK_R)

# ---------------- cavity (profile in XZ, cut from the open back) ----------------
xp = W / 2.0 - WALL_XP          # +X inner face (upper part)
xq = xp - BLOCK_T               # +X inner face (lower thick part)
xm = -(W / 2.0 - WALL_XN)       # -X inner face (thin)
xr = xm + RIB_T                 # -X rib face
zt = BODY_H / 2.0 - WALL_TB
zb = -zt

pts = [
    (xr, zt),
    (xp - POST_W, zt),
    (xp - POST_W, POST_Z0),
    (xp, POST_Z0 - POST_W),
    (xp, BLOCK_TOP),
    (xq, BLOCK_TOP - BLOCK_CH),
    (xq, zb + BOT_CH),
    (xq - BOT_CH, zb),
    (xr, zb),
]
# -X side going up, with notches into the thick wall
for (r0, r1) in NOTCHES_XN:
    pts += [(xr, r0), (xm, r0), (xm, r1), (xr, r1)]

cav_depth = D - FLOOR
cavity = (
    cq.Workplane("XZ", origin=(0, D / 2.0, 0))
    .polyline(pts)
    .close()
    .extrude(cav_depth)
)
body = body.cut(cavity)

# gusset next to the corner post
gus = (
    cq.Workplane("XZ", origin=(0, -D / 2.0 + FLOOR - 0.01, 0))
    .polyline([(xp - POST_W + 0.01, zt + 0.01),
               (xp - POST_W + 0.01, zt - GUS_Z),
               (xp - POST_W - GUS_X, zt + 0.01)])
    .close()
    .extrude(-(D - FLOOR - GUS_SINK + 0.01))
)
body = body.union(gus)

# ---------------- standoffs ----------------
floor_y = -D / 2.0 + FLOOR
for (bx, bz) in BOSS_POS:
    boss = (
        cq.Workplane("XZ", origin=(0, floor_y + BOSS_H, 0))
        .center(bx, bz)
        .circle(BOSS_OD / 2.0)
        .extrude(BOSS_H + 0.2)
    )
    body = body.union(boss)
    hole = (
        cq.Workplane("XZ", origin=(0, floor_y + BOSS_H, 0))
        .center(bx, bz)
        .circle(BOSS_ID / 2.0)
        .extrude(BOSS_H)
    )
    body = body.cut(hole)
    csk = (
        cq.Workplane("XZ", origin=(0, floor_y + BOSS_H, 0))
        .center(bx, bz)
        .circle(BOSS_ID / 2.0 + BOSS_CH)
        .workplane(offset=BOSS_CH)
        .circle(BOSS_ID / 2.0)
        .loft()
    )
    body = body.cut(csk)

# ---------------- chamfered screw holes in the lobes ----------------
hole_pts = [(sx * x_lobe, sz * HOLE_Z) for sx in (1, -1) for sz in (1, -1)]
back = cq.Workplane("XZ", origin=(0, D / 2.0, 0))
holes = back.pushPoints(hole_pts).circle(HOLE_D / 2.0).extrude(HOLE_DEPTH)
body = body.cut(holes)
for (hx, hz) in hole_pts:
    cone = (
        cq.Workplane("XZ", origin=(0, D / 2.0 + 0.01, 0))
        .center(hx, hz)
        .circle(HOLE_D / 2.0 + HOLE_CH + 0.01)
        .workplane(offset=HOLE_CH + 0.01)
        .circle(HOLE_D / 2.0)
        .loft()
    )
    body = body.cut(cone)

# ---------------- port in -X end face ----------------
endwp = cq.Workplane("YZ", origin=(-W / 2.0, 0, 0))
port_rec = (
    endwp.center(0, PORT_Z)
    .sketch()
    .rect(PORT_OUT[0], PORT_OUT[1])
    .vertices()
    .fillet(PORT_OUT_R)
    .finalize()
    .extrude(PORT_OUT_DEPTH)
)
port_thru = (
    endwp.center(0, PORT_Z)
    .sketch()
    .rect(PORT_IN[0], PORT_IN[1])
    .vertices()
    .fillet(PORT_IN_R)
    .finalize()
    .extrude(WALL_XN + RIB_T + 2.0)
)
body = body.cut(port_rec).cut(port_thru)

# ---------------- tiny corner marks in the front face ----------------
front = cq.Workplane("XZ", origin=(0, -D / 2.0, 0))
for sz in (1, -1):
    z0 = sz * (zt - 0.05)
    tri = (
        front.polyline(
            [(xr + 0.05, z0), (xr + 0.05 + MARK_LEG, z0), (xr + 0.05, z0 - sz * MARK_LEG)]
        )
        .close()
        .extrude(-MARK_DEPTH)
    )
    body = body.cut(tri)

result = body
